import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # length along X
D = 60.0           # depth along Y (front face at -Y, back face at +Y)
H = 60.0           # height along Z
R_TOP = 34.0       # big rounding of the front-top edge

# front push-button dimple
BTN_Z = 16.0        # height of the button centre above the base
BTN_D = 10.0        # flat disc diameter
DIMPLE_D = 18.2     # outer diameter of the dished surround
DIMPLE_DEPTH = 2.2  # depth of the flat disc below the front face
DISC_STEP = 0.4     # small vertical step around the disc

# back pocket (seen from the back: rounded rectangle; sharp rim at the ends,
# rolled-over rim along the top and bottom edges)
SIDE_WALL = 6.0     # rim width at the left/right ends
POCKET_DEPTH = 16.0
END_RX = 26.0       # blend floor -> left/right end walls: run along X
END_RY = 16.0       # ... and run along Y (full pocket depth)
END_R1 = 9.8        # tight radius next to the end wall (two-arc, ellipse-like blend)
CORNER_R_TOP = 6.4  # corner radii of the pocket outline on the back face
CORNER_R_BOT = 5.7
OPEN_Z0 = 3.0       # bottom of the opening on the back face
OPEN_Z1 = 56.2      # top of the opening on the back face
RIM_R_BOT = 3.8     # convex roll of the bottom rim
RIM_R_TOP = 2.0     # convex roll of the top rim
FLOOR_R_BOT = 10.0  # fillet floor -> bottom wall
FLOOR_R_TOP = 10.0  # fillet floor -> top wall

# mounting-plate seat inside the pocket
PAD_W = 36.6
PAD_Z0 = 21.0       # bottom of the seat
PAD_Z1 = 50.0       # top of the seat (runs up into the pocket top fillet)
PAD_DEPTH = 1.6
HOLE_D = 3.4
HOLE_DX = 13.0      # holes at +/- HOLE_DX
HOLE_Z = 41.3
HOLE_DEPTH = 8.0
NOTCH_W = 18.0
NOTCH_Z0 = 30.5
NOTCH_DEPTH = 7.5

VIEW = {"azimuth": 45, "elevation": 26}

YB = D / 2                      # back face plane
YF = -D / 2                     # front face plane
Y_FLOOR = YB - POCKET_DEPTH     # pocket floor plane

# ---------------- main body ----------------
body = cq.Workplane("XY").box(L, D, H).translate((0, 0, H / 2))
body = body.edges("|X and <Y and >Z").fillet(R_TOP)

# ---------------- back pocket ----------------
PX = L / 2 - SIDE_WALL                 # half length of pocket
ZB = OPEN_Z0 + RIM_R_BOT               # bottom wall of pocket
ZT = OPEN_Z1 - RIM_R_TOP               # top wall of pocket
YE = YB + 5.0                          # cutters run out past the back face

# plan section (XY): end walls blended into the floor by a two-radius
# (ellipse-like) curve, extruded along Z
r1 = END_R1
r2 = ((END_RX - r1) ** 2 + END_RY ** 2 - r1 ** 2) / (2 * (END_RY - r1))
c1 = (PX - r1, Y_FLOOR + END_RY)            # centre of the tight arc (right end)
c2 = (PX - END_RX, Y_FLOOR + r2)            # centre of the flat arc (right end)
ux, uy = c1[0] - c2[0], c1[1] - c2[1]
ul = math.hypot(ux, uy)
tp = (c2[0] + r2 * ux / ul, c2[1] + r2 * uy / ul)   # tangent point of the two arcs


def _arc_mid(c, r, p, q):
    """mid point of the short arc of centre c / radius r from p to q"""
    mx, my = (p[0] + q[0]) / 2 - c[0], (p[1] + q[1]) / 2 - c[1]
    ml = math.hypot(mx, my)
    return (c[0] + r * mx / ml, c[1] + r * my / ml)


def _mx(p):
    return (-p[0], p[1])


w_top = (PX, Y_FLOOR + END_RY)
f_end = (PX - END_RX, Y_FLOOR)
m1 = _arc_mid(c1, r1, w_top, tp)
m2 = _arc_mid(c2, r2, tp, f_end)
cut_ends = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .moveTo(-PX, YE)
    .lineTo(*_mx(w_top))
    .threePointArc(_mx(m1), _mx(tp))
    .threePointArc(_mx(m2), _mx(f_end))
    .lineTo(*f_end)
    .threePointArc(m2, tp)
    .threePointArc(m1, w_top)
    .lineTo(PX, YE)
    .close()
    .extrude(H + 2.0)
)
# side section (YZ): floor, floor fillets, walls and rolled rims, extruded along X
cut_sides = (
    cq.Workplane("YZ", origin=(-L / 2 - 1.0, 0, 0))
    .moveTo(YE, OPEN_Z0)
    .lineTo(YB, OPEN_Z0)
    .radiusArc((YB - RIM_R_BOT, ZB), -RIM_R_BOT)
    .lineTo(Y_FLOOR + FLOOR_R_BOT, ZB)
    .radiusArc((Y_FLOOR, ZB + FLOOR_R_BOT), FLOOR_R_BOT)
    .lineTo(Y_FLOOR, ZT - FLOOR_R_TOP)
    .radiusArc((Y_FLOOR + FLOOR_R_TOP, ZT), FLOOR_R_TOP)
    .lineTo(YB - RIM_R_TOP, ZT)
    .radiusArc((YB, OPEN_Z1), -RIM_R_TOP)
    .lineTo(YE, OPEN_Z1)
    .close()
    .extrude(L + 2.0)
)
# back-face outline (XZ): rounded rectangle, extruded along Y


def _corner_mid(cx, cz, r, ang_deg):
    return (cx + r * math.cos(math.radians(ang_deg)), cz + r * math.sin(math.radians(ang_deg)))


rt, rb = CORNER_R_TOP, CORNER_R_BOT
cut_outline = (
    cq.Workplane("XZ", origin=(0, YE, 0))
    .moveTo(-PX + rb, OPEN_Z0)
    .lineTo(PX - rb, OPEN_Z0)
    .threePointArc(_corner_mid(PX - rb, OPEN_Z0 + rb, rb, -45), (PX, OPEN_Z0 + rb))
    .lineTo(PX, OPEN_Z1 - rt)
    .threePointArc(_corner_mid(PX - rt, OPEN_Z1 - rt, rt, 45), (PX - rt, OPEN_Z1))
    .lineTo(-PX + rt, OPEN_Z1)
    .threePointArc(_corner_mid(-PX + rt, OPEN_Z1 - rt, rt, 135), (-PX, OPEN_Z1 - rt))
    .lineTo(-PX, OPEN_Z0 + rb)
    .threePointArc(_corner_mid(-PX + rb, OPEN_Z0 + rb, rb, 225), (-PX + rb, OPEN_Z0))
    .close()
    .extrude(YE - Y_FLOOR + 2.0)
)
pocket = cut_ends.intersect(cut_sides).intersect(cut_outline)
body = body.cut(pocket)

# mounting-plate seat, screw holes and the deeper notch
pad = (
    cq.Workplane("XY")
    .box(PAD_W, PAD_DEPTH + 10.0, PAD_Z1 - PAD_Z0)
    .translate((0, Y_FLOOR - PAD_DEPTH + (PAD_DEPTH + 10.0) / 2, (PAD_Z0 + PAD_Z1) / 2))
)
body = body.cut(pad)
Y_PAD = Y_FLOOR - PAD_DEPTH
notch = (
    cq.Workplane("XY")
    .box(NOTCH_W, NOTCH_DEPTH + 1.0, PAD_Z1 - NOTCH_Z0)
    .translate((0, Y_PAD - NOTCH_DEPTH + (NOTCH_DEPTH + 1.0) / 2, (NOTCH_Z0 + PAD_Z1) / 2))
)
body = body.cut(notch)
holes = (
    cq.Workplane("XZ", origin=(0, Y_PAD, 0))
    .pushPoints([(HOLE_DX, HOLE_Z), (-HOLE_DX, HOLE_Z)])
    .circle(HOLE_D / 2)
    .extrude(HOLE_DEPTH)
)
body = body.cut(holes)

# ---------------- front dimple + button disc ----------------
# revolved profile: flat disc recessed DIMPLE_DEPTH behind a small step, the
# surround dished by an arc that runs out tangentially into the front face at
# DIMPLE_D/2 (profile drawn in the +X half plane, so the seam lies along +X).
r_in = BTN_D / 2
r_out = DIMPLE_D / 2
dish = DIMPLE_DEPTH - DISC_STEP       # depth reached by the dished surround
r_arc = ((r_out - r_in) ** 2 + dish ** 2) / (2 * dish)
cy = YF + r_arc                       # arc centre (r_out, cy)
a0 = -math.pi / 2
a1 = math.atan2((YF + dish) - cy, r_in - r_out)
am = 0.5 * (a0 + a1)
mid = (r_out + r_arc * math.cos(am), cy + r_arc * math.sin(am))
dimple = (
    cq.Workplane("XY", origin=(0, 0, BTN_Z))
    .moveTo(0, YF - 1.0)
    .lineTo(r_out, YF - 1.0)
    .lineTo(r_out, YF)
    .threePointArc(mid, (r_in, YF + dish))
    .lineTo(r_in, YF + DIMPLE_DEPTH)
    .lineTo(0, YF + DIMPLE_DEPTH)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.cut(dimple)

result = body
